import math
import cadquery as cq

# ------------------------------------------------------------------
# Kinematic mount for a rectangular optic on a pedestal post.
#   front plate : optic holder with front pocket + clear aperture
#   back plate  : L-shaped fixed plate sitting on the post
#   adjusters   : two ball-tipped adjuster screws (top-left, bottom-right)
# Driving dimensions are given in "units" and scaled by U to millimetres.
# X: left/right, Y: front(-)/back(+), Z: up.  Post axis at X=Y=0.
# ------------------------------------------------------------------
U = 0.5  # mm per unit

# ---- post -------------------------------------------------------
FLANGE_D = 65.5
FLANGE_H = 9.9
POST_D = 51.5
POST_TOP = 102.7

# ---- front plate (optic holder) --------------------------------
FP_Y_FRONT = -31.6
FP_Y_BACK_THIN = -18.4
FP_Y_BACK_THICK = -13.6
FP_X_L = -79.3
FP_X_R = 43.6
FP_LOBE_X = 51.0          # bottom-right lobe (carries the lower adjuster contact)
FP_LOBE_Z = (7.9, 17.4, 26.9)   # lobe break points above the plate bottom
FP_LOBE_BOT_X = 44.8
FP_CORNER_CH = 4.3        # bottom-left corner chamfer
FP_Z_BOT = 105.7
FP_Z_TOP = 215.7          # main top edge
TAB_Z_TOP = 235.9         # top of the top-left tab
TAB_X_R = -53.4
TAB_CH_L = (7.4, 7.5)     # tab corner chamfers (dx, dz)
TAB_CH_R = (8.9, 7.5)
TAB_FILLET = 7.0
FP_EDGE_CH = 1.0
THICK_X_L = -44.5         # thick (back) region of the holder
THICK_Z_BOT = 136.0

POCKET_X_L = -53.5
POCKET_Z_BOT = 145.0
POCKET_Z_BOT_SIDE = 146.5
POCKET_Z_TOP = 200.4
POCKET_Y_FLOOR = -19.8
SEAT_DEPTH = 3.5
DB_D = 6.5          # dog-bone corner reliefs of the optic seat
DB_OFF = 1.0

AP_R = 1.6          # corner rounding of the aperture outline
POCKET_R = 4.0
AP_X_L = -42.35
AP_X_R = 40.1
AP_Z_BOT = 153.2
AP_Z_TOP = 193.8
AP_TAB_Z_TOP = 199.9
AP_TAB_Z_BOT = 148.45

# ---- back plate (fixed, L-shaped) ------------------------------
BP_Y_FRONT = -10.6
BP_Y_BACK = 10.4
BP_X_L = -79.3
BP_BULGE_X = -82.3        # outer side of the column bows out slightly
BP_BULGE_Z = (145.0, 203.5)
BP_END_CH = (5.0, 7.5)    # chamfers of the bar end (bottom, top)
BP_LOBE_CH = 6.5
BP_X_R = 51.5
BP_Z_BOT = 105.7
BP_Z_TOP = 235.9
BP_BAR_TOP = 131.5
BP_COL_X = -52.5
BP_FILLET = 10.0
BP_EDGE_CH = 1.0
SPH_C = (-32.4, 34.5, 173.0)   # spherical relief in the column's inner face
SPH_R = 43.0
CROSS_Z = 173.0
CROSS_CB_D = 16.0     # counterbore of the cross hole, seen inside the relief
CROSS_CB_X = -67.0
FOOT_W = 59.4

# ---- adjusters -------------------------------------------------
ADJ_D = 12.6
ADJ_BACK = 25.1
ADJ_BALL_D = 14.0
ADJ_BALL_Y = -14.5
ADJ_TOP = (-66.2, 225.1)
ADJ_BOT = (40.1, 118.45)

# spring holes (keyholes) shared by both plates: x, z, slot angle
KEYHOLES = [(-66.1, 205.0, 0.0), (-56.2, 129.35, -45.0), (19.4, 120.35, 90.0)]
KEY_D = 10.0
KEY_SLOT_L = 21.6      # overall length of the pin groove
KEY_BULB_D = 5.0       # round ends of the groove
KEY_NECK_W = 4.6
KEY_SLOT_DEPTH = 2.0


def s(v):
    return v * U


def xz_profile(start, segs, y0, depth):
    """Closed XZ profile at Y=y0 extruded towards -Y by depth.
    segs: ('L', x, z) line or ('A', xm, zm, x, z) three-point arc."""
    w = cq.Workplane("XZ", origin=(0, s(y0), 0)).moveTo(s(start[0]), s(start[1]))
    for sg in segs:
        if sg[0] == "L":
            w = w.lineTo(s(sg[1]), s(sg[2]))
        else:
            w = w.threePointArc((s(sg[1]), s(sg[2])), (s(sg[3]), s(sg[4])))
    return w.close().extrude(s(depth))


def xz_poly(pts, y0, depth):
    return xz_profile(pts[0], [("L", x, z) for x, z in pts[1:]], y0, depth)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(s(x1 - x0), s(y1 - y0), s(z1 - z0), centered=False)
            .translate((s(x0), s(y0), s(z0))))


def ycyl(x, z, d, y0, y1):
    return (cq.Workplane("XZ", origin=(s(x), s(y1), s(z)))
            .circle(s(d) / 2).extrude(s(y1 - y0)))


def bowtie_y(x, z, ang, y0, y1):
    """spring-pin groove: two round ends joined by a narrower neck"""
    off = KEY_SLOT_L / 2 - KEY_BULB_D / 2
    wp = (cq.Workplane("XZ", origin=(s(x), s(y1), s(z)))
          .transformed(rotate=(0, 0, ang)))
    g = wp.rect(s(2 * off), s(KEY_NECK_W)).extrude(s(y1 - y0))
    g = g.union(wp.pushPoints([(s(-off), 0), (s(off), 0)])
                .circle(s(KEY_BULB_D) / 2).extrude(s(y1 - y0)))
    return g


def fillet_pt(r):
    """mid point of a 90 deg fillet arc (helper for three-point arcs)"""
    return r * (1 - math.cos(math.radians(45)))


# ================= post =========================================
post = (cq.Workplane("XY").circle(s(FLANGE_D) / 2).extrude(s(FLANGE_H))
        .faces(">Z").workplane().circle(s(POST_D) / 2)
        .extrude(s(POST_TOP - FLANGE_H)))
post = post.rotate((0, 0, 0), (0, 0, 1), 180)

# ================= front plate ==================================
fr = fillet_pt(TAB_FILLET)
fp = xz_profile(
    (FP_X_L + FP_CORNER_CH, FP_Z_BOT),
    [("L", FP_LOBE_BOT_X, FP_Z_BOT),
     ("L", FP_LOBE_X, FP_Z_BOT + FP_LOBE_Z[0]),
     ("L", FP_LOBE_X, FP_Z_BOT + FP_LOBE_Z[1]),
     ("L", FP_X_R, FP_Z_BOT + FP_LOBE_Z[2]),
     ("L", FP_X_R, FP_Z_TOP),
     ("L", TAB_X_R + TAB_FILLET, FP_Z_TOP),
     ("A", TAB_X_R + fr, FP_Z_TOP + fr, TAB_X_R, FP_Z_TOP + TAB_FILLET),
     ("L", TAB_X_R, TAB_Z_TOP - TAB_CH_R[1]),
     ("L", TAB_X_R - TAB_CH_R[0], TAB_Z_TOP),
     ("L", FP_X_L + TAB_CH_L[0], TAB_Z_TOP),
     ("L", FP_X_L, TAB_Z_TOP - TAB_CH_L[1]),
     ("L", FP_X_L, FP_Z_BOT + FP_CORNER_CH)],
    FP_Y_BACK_THIN, FP_Y_BACK_THIN - FP_Y_FRONT)
fp = fp.faces("<Y").chamfer(s(FP_EDGE_CH))

thick = xz_poly([(THICK_X_L, THICK_Z_BOT), (FP_X_R, THICK_Z_BOT),
                 (FP_X_R, FP_Z_TOP), (THICK_X_L, FP_Z_TOP)],
                FP_Y_BACK_THICK, FP_Y_BACK_THICK - FP_Y_BACK_THIN + 0.01)
fp = fp.union(thick)

# front pocket, open on the +X side, bottom edge follows the aperture relief
pk = xz_poly([(POCKET_X_L, POCKET_Z_BOT_SIDE), (-33.0, POCKET_Z_BOT_SIDE),
              (-25.0, POCKET_Z_BOT), (24.0, POCKET_Z_BOT),
              (32.0, POCKET_Z_BOT_SIDE), (FP_LOBE_X + 5, POCKET_Z_BOT_SIDE),
              (FP_LOBE_X + 5, POCKET_Z_TOP), (POCKET_X_L, POCKET_Z_TOP)],
             POCKET_Y_FLOOR, POCKET_Y_FLOOR - FP_Y_FRONT + 5)
pk = pk.edges("|Y").fillet(s(POCKET_R))
fp = fp.cut(pk)
# corner reliefs of the pocket
for zc in (POCKET_Z_BOT_SIDE + 0.8, POCKET_Z_TOP - 0.8):
    fp = fp.cut(ycyl(POCKET_X_L + 0.8, zc, 4.0, FP_Y_FRONT - 1, POCKET_Y_FLOOR))

# through aperture with relief tabs top and bottom
ap_pts = [
    (AP_X_L, AP_Z_BOT), (-31.0, AP_Z_BOT), (-26.5, AP_TAB_Z_BOT),
    (24.8, AP_TAB_Z_BOT), (29.3, AP_Z_BOT), (AP_X_R, AP_Z_BOT),
    (AP_X_R, AP_Z_TOP), (30.2, AP_Z_TOP), (26.6, AP_TAB_Z_TOP),
    (-27.4, AP_TAB_Z_TOP), (-31.0, AP_Z_TOP), (AP_X_L, AP_Z_TOP),
]
ap = xz_poly(ap_pts, 0, 40).edges("|Y").fillet(s(AP_R))
fp = fp.cut(ap)
# dog-bone reliefs at the optic seat corners (from the back)
for (cx, cz) in ((AP_X_L - DB_OFF, AP_Z_BOT - DB_OFF), (AP_X_L - DB_OFF, AP_Z_TOP + DB_OFF),
                 (AP_X_R - 0.8, AP_Z_BOT - DB_OFF), (AP_X_R - 0.8, AP_Z_TOP + DB_OFF)):
    fp = fp.cut(ycyl(cx, cz, DB_D, FP_Y_BACK_THICK - SEAT_DEPTH, 0))

# spring holes + pin grooves on the front face
for (kx, kz, ka) in KEYHOLES:
    fp = fp.cut(ycyl(kx, kz, KEY_D, -40, 0))
    fp = fp.cut(bowtie_y(kx, kz, ka, FP_Y_FRONT - 1, FP_Y_FRONT + KEY_SLOT_DEPTH))

# small holes on the front face
fp = fp.cut(ycyl(-33.2, 140.45, 3.4, FP_Y_FRONT - 1, FP_Y_FRONT + 6))
fp = fp.cut(ycyl(31.6, 206.65, 3.6, FP_Y_FRONT - 1, FP_Y_FRONT + 6))

# clamp screw hole in the top bar (countersunk)
TB_HOLE = (-6.2, -24.0)
fp = fp.cut(cq.Workplane("XY", origin=(s(TB_HOLE[0]), s(TB_HOLE[1]), s(FP_Z_TOP + 1)))
            .circle(s(7.8) / 2).extrude(-s(FP_Z_TOP - POCKET_Z_TOP + 3)))
fp = fp.cut(cq.Workplane("XY").add(cq.Solid.makeCone(
    s(3.9), s(6.0), s(2.1),
    pnt=cq.Vector(s(TB_HOLE[0]), s(TB_HOLE[1]), s(FP_Z_TOP - 1.1)),
    dir=cq.Vector(0, 0, 1))))

# ================= back plate ===================================
br = fillet_pt(BP_FILLET)
bp = xz_profile(
    (BP_X_L + FP_CORNER_CH, BP_Z_BOT),
    [("L", BP_X_R - BP_END_CH[0], BP_Z_BOT),
     ("L", BP_X_R, BP_Z_BOT + BP_END_CH[0]),
     ("L", BP_X_R, BP_BAR_TOP - BP_END_CH[1]),
     ("L", BP_X_R - BP_END_CH[1], BP_BAR_TOP),
     ("L", BP_COL_X + BP_FILLET, BP_BAR_TOP),
     ("A", BP_COL_X + br, BP_BAR_TOP + br, BP_COL_X, BP_BAR_TOP + BP_FILLET),
     ("L", BP_COL_X, BP_Z_TOP - BP_LOBE_CH),
     ("L", BP_COL_X - BP_LOBE_CH, BP_Z_TOP),
     ("L", BP_X_L + BP_LOBE_CH, BP_Z_TOP),
     ("L", BP_X_L, BP_Z_TOP - BP_LOBE_CH),
     ("L", BP_X_L, BP_BULGE_Z[1]),
     ("A", BP_BULGE_X, sum(BP_BULGE_Z) / 2, BP_X_L, BP_BULGE_Z[0]),
     ("L", BP_X_L, BP_Z_BOT + FP_CORNER_CH)],
    BP_Y_BACK, BP_Y_BACK - BP_Y_FRONT)
bp = bp.faces(">Y").chamfer(s(BP_EDGE_CH))
bp = bp.faces("<Y").chamfer(s(BP_EDGE_CH))
# tapered foot under the back plate sitting on the post (two-section ruled loft)
foot = (cq.Workplane("XY", origin=(0, s((BP_Y_FRONT + BP_Y_BACK) / 2), s(POST_TOP)))
        .rect(s(POST_D), s(BP_Y_BACK - BP_Y_FRONT - 3.0))
        .workplane(offset=s(BP_Z_BOT - POST_TOP + 0.01))
        .rect(s(FOOT_W), s(BP_Y_BACK - BP_Y_FRONT))
        .loft(ruled=True))
bp = bp.union(foot)

# spherical relief cut into the column (open towards the back)
sph = cq.Workplane("XY").sphere(s(SPH_R)).translate(tuple(s(v) for v in SPH_C))
bp = bp.cut(sph)

# spring holes + grooves on the back face
for (kx, kz, ka) in KEYHOLES:
    bp = bp.cut(ycyl(kx, kz, KEY_D, BP_Y_FRONT - 1, BP_Y_BACK + 1))
    bp = bp.cut(bowtie_y(kx, kz, ka, BP_Y_BACK - KEY_SLOT_DEPTH, BP_Y_BACK + 1))

# cross hole through the column (X direction) with counterbore on the inside
bp = bp.cut(cq.Workplane("YZ", origin=(s(BP_BULGE_X - 1), 0, s(CROSS_Z)))
            .circle(s(7.7) / 2).extrude(s(40)))
bp = bp.cut(cq.Workplane("YZ", origin=(s(CROSS_CB_X), 0, s(CROSS_Z)))
            .circle(s(CROSS_CB_D) / 2).extrude(s(25)))
# post screw counterbore in the top of the bar
bp = bp.cut(cq.Workplane("XY", origin=(0, 0, s(BP_BAR_TOP)))
            .circle(s(10.0) / 2).extrude(-s(BP_BAR_TOP - POST_TOP + 1)))
bp = bp.cut(cq.Workplane("XY", origin=(0, 0, s(BP_BAR_TOP)))
            .circle(s(16.9) / 2).extrude(-s(6.0)))

# ================= adjusters ====================================
adjs = None
for (ax, az) in (ADJ_TOP, ADJ_BOT):
    a = ycyl(ax, az, ADJ_D, BP_Y_FRONT - 1.5, ADJ_BACK)
    a = a.union(cq.Workplane("XY").sphere(s(ADJ_BALL_D) / 2)
                .translate((s(ax), s(ADJ_BALL_Y), s(az))))
    a = a.faces(">Y").edges().fillet(s(0.8))
    a = a.cut(cq.Workplane("XZ", origin=(s(ax), s(ADJ_BACK), s(az)))
              .polygon(6, s(5.0)).extrude(s(3.0)))
    adjs = a if adjs is None else adjs.union(a)

result = post.union(bp).union(fp).union(adjs)
